import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BASE_D = 240.0          # base disc diameter
BASE_T = 20.0           # base disc thickness
BASE_FILLET = 3.0       # rounded top edge of the base

COL_W = 120.0           # column width (X)
COL_T = 20.0            # column thickness (Y)
COL_TOP = 420.0         # column top height (Z)

PLATE_W = 240.0         # mounting plate width (X)
PLATE_H = 120.0         # mounting plate height (Z)
PLATE_T = 20.0          # mounting plate thickness (Y)
PLATE_TOP = 520.0       # top of plate (Z)
PLATE_FILLET = 3.0      # small round on all plate edges

BIG_HOLE_D = 60.0       # central cable hole
SMALL_HOLE_D = 12.0     # four fixing holes in the plate
SMALL_HOLE_EDGE = 16.0  # distance from plate side edge to hole centre
SMALL_HOLE_DZ = 40.0    # vertical pitch of the fixing holes

BASE_HOLE_D = 9.0       # cross pattern of holes in the base
BASE_HOLE_PITCH = 12.0
BASE_HOLES_PER_ARM = 5

ORIGIN = cq.Vector(0, 0, 0)
ZAXIS = cq.Vector(0, 0, 1)
XAXIS = cq.Vector(1, 0, 0)


def y_cylinder(d, length, x, z):
    """Cylinder along Y (seam placed on the top side, out of sight)."""
    c = cq.Solid.makeCylinder(d / 2.0, length, cq.Vector(0, 0, -length / 2.0), ZAXIS)
    c = c.rotate(ORIGIN, ZAXIS, -90).rotate(ORIGIN, XAXIS, -90)
    return c.translate(cq.Vector(x, 0, z))


def z_cylinder(d, length, x, y, seam_deg=90.0):
    """Cylinder along Z, seam turned to the back (+Y) side."""
    c = cq.Solid.makeCylinder(d / 2.0, length, cq.Vector(0, 0, -length / 2.0), ZAXIS)
    return c.rotate(ORIGIN, ZAXIS, seam_deg).translate(cq.Vector(x, y, 0))


# ---------------- base disc ----------------
base = (
    cq.Workplane("XY")
    .circle(BASE_D / 2.0)
    .extrude(BASE_T)
    .rotate((0, 0, 0), (0, 0, 1), 90)   # keep the cylinder seam out of the front views
    .faces(">Z").edges()
    .fillet(BASE_FILLET)
)

base_cutters = []
for i in range(1, BASE_HOLES_PER_ARM + 1):
    r = i * BASE_HOLE_PITCH
    for (x, y) in ((r, 0), (-r, 0), (0, r), (0, -r)):
        base_cutters.append(z_cylinder(BASE_HOLE_D, BASE_T * 4, x, y))
base = base.cut(cq.Workplane("XY").newObject([cq.Compound.makeCompound(base_cutters)]))

# ---------------- column ----------------
column = (
    cq.Workplane("XY")
    .box(COL_W, COL_T, COL_TOP - BASE_T, centered=(True, True, False))
    .translate((0, 0, BASE_T))
)

# ---------------- mounting plate (in front of the column, -Y side) ----------------
plate_cy = -COL_T / 2.0 - PLATE_T / 2.0
plate_cz = PLATE_TOP - PLATE_H / 2.0
hx = PLATE_W / 2.0 - SMALL_HOLE_EDGE
hz = SMALL_HOLE_DZ / 2.0

plate = (
    cq.Workplane("XZ")
    .rect(PLATE_W, PLATE_H)
    .extrude(PLATE_T / 2.0, both=True)
    .edges()
    .fillet(PLATE_FILLET)
)
plate_cutters = [y_cylinder(BIG_HOLE_D, PLATE_T * 4, 0, 0)]
for sx in (-1, 1):
    for sz in (-1, 1):
        plate_cutters.append(y_cylinder(SMALL_HOLE_D, PLATE_T * 4, sx * hx, sz * hz))
plate = plate.cut(cq.Workplane("XY").newObject([cq.Compound.makeCompound(plate_cutters)]))
plate = plate.translate((0, plate_cy, plate_cz))

result = base.union(column).union(plate)

VIEW = {"azimuth": 45, "elevation": 26}
